import math
import cadquery as cq

VIEW = {"azimuth": 45, "elevation": 26}

# ------------------------------------------------------------------
# Cover / lid: rounded rectangular shell open at the bottom, with an
# inset locating lip, two cable arches in the front wall, a notch in
# the left wall, a through hole in the top and a screw boss hanging
# from the underside of the top plate.
# ------------------------------------------------------------------

# ---------------- driving dimensions (mm) ----------------
W = 80.5           # overall width  (X)
D = 100.0          # overall depth  (Y)
H_WALL = 12.0      # outer wall height (top face down to the step)
LIP_H = 3.0        # height of the inset lip below the wall
R_CORNER = 4.2     # vertical corner radius of the outer wall
T_TOP = 2.2        # top plate thickness
T_WALL = 4.0       # side wall thickness
LIP_INSET = 2.4    # lip inset from the outer wall face
R_LIP = 2.0        # vertical corner radius of the lip
R_INNER = 1.5      # vertical corner radius inside the cavity
H = H_WALL + LIP_H # total height of the shell

# through hole in the top plate (front-right corner)
HOLE_X = 25.5
HOLE_Y = -35.15
HOLE_D = 9.7

# U-shaped cable arches in the front wall (semicircle centred on the step line)
ARCH_R = 8.25
ARCH_XS = [-21.9, 5.45]

# rectangular notch in the left wall (open to the bottom)
NOTCH_Y0 = -0.4
NOTCH_Y1 = 22.4
NOTCH_H = 8.6      # measured from the bottom of the lip

# screw boss hanging from the underside of the top plate
BOSS_X = 0.8
BOSS_Y = 13.0
BOSS_D = 10.0
BOSS_BELOW = 6.0       # protrusion below the bottom of the lip
BOSS_FILLET = 3.0      # root fillet to the ceiling
BOSS_HOLE_D = 3.0      # pilot hole in the tip
BOSS_HOLE_DEPTH = 10.0

# ---------------- outer shell ----------------
outer = (cq.Workplane("XY").workplane(offset=LIP_H)
         .rect(W, D).extrude(H_WALL)
         .edges("|Z").fillet(R_CORNER))
lip = (cq.Workplane("XY")
       .rect(W - 2 * LIP_INSET, D - 2 * LIP_INSET).extrude(LIP_H + 0.01)
       .edges("|Z").fillet(R_LIP))
body = outer.union(lip)

# hollow it out from below (open bottom, plate of T_TOP on top)
cavity = (cq.Workplane("XY").workplane(offset=-1)
          .rect(W - 2 * T_WALL, D - 2 * T_WALL).extrude(H - T_TOP + 1)
          .edges("|Z").fillet(R_INNER))
body = body.cut(cavity)

# ---------------- screw boss (revolved, root fillet included) ----------------
z_ceil = H - T_TOP
z_tip = -BOSS_BELOW
r_b = BOSS_D / 2
f = BOSS_FILLET
c45 = math.cos(math.radians(45))
# profile drawn in the YZ plane (local x = world Y, local y = world Z)
boss = (cq.Workplane("YZ")
        .moveTo(0, z_tip)
        .lineTo(r_b, z_tip)
        .lineTo(r_b, z_ceil - f)
        .threePointArc((r_b + f - f * c45, z_ceil - f + f * c45), (r_b + f, z_ceil))
        .lineTo(r_b + f, z_ceil + 0.5)
        .lineTo(0, z_ceil + 0.5)
        .close()
        .revolve(360, (0, 0, 0), (0, 1, 0))
        .translate((BOSS_X, BOSS_Y, 0)))
body = body.union(boss)

# pilot hole in the boss tip
body = body.cut(cq.Workplane("XY").workplane(offset=z_tip - 1)
                .center(BOSS_X, BOSS_Y).circle(BOSS_HOLE_D / 2)
                .extrude(BOSS_HOLE_DEPTH + 1))

# ---------------- top through hole ----------------
body = body.cut(cq.Workplane("XY").workplane(offset=-1)
                .center(HOLE_X, HOLE_Y).circle(HOLE_D / 2).extrude(H + 2))

# ---------------- cable arches in the front wall ----------------
# (XZ workplane normal is -Y, so offset places the sketch just inside the wall)
for ax in ARCH_XS:
    wp = cq.Workplane("XZ").workplane(offset=D / 2 - T_WALL - 1)
    arch = wp.center(ax, LIP_H).circle(ARCH_R).extrude(T_WALL + 2)
    slot = (cq.Workplane("XZ").workplane(offset=D / 2 - T_WALL - 1)
            .center(ax, (LIP_H - 1) / 2).rect(2 * ARCH_R, LIP_H + 1)
            .extrude(T_WALL + 2))
    body = body.cut(arch).cut(slot)

# ---------------- notch in the left wall ----------------
notch = (cq.Workplane("XY").workplane(offset=-1)
         .center(-W / 2 + T_WALL / 2, (NOTCH_Y0 + NOTCH_Y1) / 2)
         .rect(T_WALL + 2, NOTCH_Y1 - NOTCH_Y0).extrude(NOTCH_H + 1))
body = body.cut(notch)

result = body
